import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R1 = 10.0          # top (vertical) boss outer radius
H1 = 17.5          # top boss height
D1_HOLE = 12.8     # top boss bore

W = 10.0           # arm width (along X)
TH = 12.5          # thickness of the horizontal arm segment (Z)
TD = 10.25         # perpendicular thickness of the inclined arm segment
ALPHA = 55.0       # inclination of the arm segment below horizontal (deg)
Y_OC = 25.45       # Y of the outer (upper) bend corner
R_BEND_OUT = 3.0   # outer bend rounding radius
R_BEND_IN = 2.0    # inner bend rounding radius

YB = 68.0          # lower boss axis position (Y)
ZB = -49.5         # lower boss axis position (Z)
R2 = 11.4          # lower boss outer radius
L2 = 17.7          # lower boss length (along X)
D2_HOLE = 15.2     # lower boss bore
BORE2_DY = 0.6     # lower bore offset from the outer arc centre (Y)
BORE2_DZ = 0.5     # lower bore offset from the outer arc centre (Z)

TOP_TAN_DEG = 96.0    # where the upper blend line touches the lower boss
R_TOP_BLEND = 3.0     # concave blend radius arm -> lower boss (top side)
BOT_TAN_DEG = 288.0   # where the lower blend arc touches the lower boss
PC_SHIFT = 0.4        # lower arm face ends this far past the boss axis

Y_T1 = 53.2        # arm starts to widen (top view)
R_TC = 6.0         # concave radius of the widening (top view)
R_TV = 1.5         # convex radius of the widening (top view)
R_ROOT = 10.0      # fillet between arm sides and the top boss


# ---------------- helpers ----------------
def v_add(a, b):
    return (a[0] + b[0], a[1] + b[1])


def v_sub(a, b):
    return (a[0] - b[0], a[1] - b[1])


def v_mul(a, s):
    return (a[0] * s, a[1] * s)


def v_dot(a, b):
    return a[0] * b[0] + a[1] * b[1]


def v_len(a):
    return math.hypot(a[0], a[1])


def v_unit(a):
    l = v_len(a)
    return (a[0] / l, a[1] / l)


def corner_round(p, h_in, h_out, r):
    """Round the corner p between incoming heading h_in and outgoing h_out.
    Returns (tangent point in, arc mid point, tangent point out)."""
    cos_t = max(-1.0, min(1.0, v_dot(h_in, h_out)))
    turn = math.acos(cos_t)
    t = r * math.tan(turn / 2.0)
    t1 = v_sub(p, v_mul(h_in, t))
    t2 = v_add(p, v_mul(h_out, t))
    # centre lies on the inner side of the turn
    cross = h_in[0] * h_out[1] - h_in[1] * h_out[0]
    if cross > 0:      # left turn
        nrm = (-h_in[1], h_in[0])
    else:              # right turn
        nrm = (h_in[1], -h_in[0])
    ctr = v_add(t1, v_mul(nrm, r))
    mid = v_add(ctr, v_mul(v_unit(v_sub(p, ctr)), r))
    return t1, mid, t2


# ---------------- side profile (Y,Z plane) ----------------
a = math.radians(ALPHA)
d = (math.cos(a), -math.sin(a))        # heading down the inclined segment
n = (math.sin(a), math.cos(a))         # outward normal of its upper face
c = (YB, ZB)

P_oc = (Y_OC, TH / 2.0)
k_top = v_dot(n, P_oc)
k_bot = k_top - TD
Y_IC = (k_bot + math.cos(a) * TH / 2.0) / math.sin(a)
P_ic = (Y_IC, -TH / 2.0)

# upper blend: tangent line to the boss circle, concave round into arm face
tt = math.radians(TOP_TAN_DEG)
T_top = (YB + R2 * math.cos(tt), ZB + R2 * math.sin(tt))
h_tan = (math.sin(tt), -math.cos(tt))
s = (k_top - v_dot(n, T_top)) / v_dot(n, h_tan)
Q = v_add(T_top, v_mul(h_tan, s))

# lower blend: corner at foot point on lower face, convex arc tangent to boss
P_c = v_add(v_sub(c, v_mul(n, v_dot(n, c) - k_bot)), v_mul(d, PC_SHIFT))
tb = math.radians(BOT_TAN_DEG)
u_b = (math.cos(tb), math.sin(tb))
T_bot = v_add(c, v_mul(u_b, R2))
# centre Cb = c - (Rb - R2) * u_b, |P_c - Cb| = Rb
w = v_sub(P_c, v_add(c, v_mul(u_b, R2)))          # P_c - T_bot
# |w + Rb*u_b|^2 = Rb^2  ->  |w|^2 + 2 Rb (w.u_b) = 0
Rb = -v_dot(w, w) / (2.0 * v_dot(w, u_b))
Cb = v_sub(T_bot, v_mul(u_b, Rb))
ang0 = math.atan2(T_bot[1] - Cb[1], T_bot[0] - Cb[0])
ang1 = math.atan2(P_c[1] - Cb[1], P_c[0] - Cb[0])
while ang1 < ang0:
    ang1 += 2 * math.pi
am = 0.5 * (ang0 + ang1)
if am - ang0 > math.pi / 2:  # choose the short way round
    ang1 -= 2 * math.pi
    am = 0.5 * (ang0 + ang1)
M_bot = (Cb[0] + Rb * math.cos(am), Cb[1] + Rb * math.sin(am))

# boss arc (clockwise from top tangent point to bottom tangent point)
a_top = tt
a_bot = tb - 2 * math.pi
M_circ = (YB + R2 * math.cos(0.5 * (a_top + a_bot)),
          ZB + R2 * math.sin(0.5 * (a_top + a_bot)))

oc1, ocm, oc2 = corner_round(P_oc, (1.0, 0.0), d, R_BEND_OUT)
q1, qm, q2 = corner_round(Q, d, h_tan, R_TOP_BLEND)
ic1, icm, ic2 = corner_round(P_ic, (-d[0], -d[1]), (-1.0, 0.0), R_BEND_IN)

side = (
    cq.Workplane("YZ")
    .moveTo(0.0, TH / 2.0)
    .lineTo(*oc1)
    .threePointArc(ocm, oc2)
    .lineTo(*q1)
    .threePointArc(qm, q2)
    .lineTo(*T_top)
    .threePointArc(M_circ, T_bot)
    .threePointArc(M_bot, P_c)
    .lineTo(*ic1)
    .threePointArc(icm, ic2)
    .lineTo(0.0, -TH / 2.0)
    .close()
    .extrude(L2, both=True)
)

# ---------------- top-view profile (X,Y plane) ----------------
hw = W / 2.0
hl = L2 / 2.0
dx = hl - hw
rr = R_TC + R_TV
Y_T2 = Y_T1 + math.sqrt(rr ** 2 - (dx - rr) ** 2)   # full boss width reached
c1 = (hw + R_TC, Y_T1)                  # concave arc centre
c2 = (hl - R_TV, Y_T2)                  # convex arc centre
u12 = v_unit(v_sub(c2, c1))
Mt = v_add(c1, v_mul(u12, R_TC))        # tangent point between the two arcs
a1s = math.pi
a1e = math.atan2(Mt[1] - c1[1], Mt[0] - c1[0])
m1 = (c1[0] + R_TC * math.cos(0.5 * (a1s + a1e)), c1[1] + R_TC * math.sin(0.5 * (a1s + a1e)))
a2s = math.atan2(Mt[1] - c2[1], Mt[0] - c2[0])
a2e = 0.0
m2 = (c2[0] + R_TV * math.cos(0.5 * (a2s + a2e)), c2[1] + R_TV * math.sin(0.5 * (a2s + a2e)))
Mx, My = Mt
Y_END = YB + R2 + 5.0

plan = (
    cq.Workplane("XY")
    .workplane(offset=ZB - R2 - 10.0)
    .moveTo(-hw, 0.0)
    .lineTo(hw, 0.0)
    .lineTo(hw, Y_T1)
    .threePointArc(m1, (Mx, My))
    .threePointArc(m2, (hl, Y_T2))
    .lineTo(hl, Y_END)
    .lineTo(-hl, Y_END)
    .lineTo(-hl, Y_T2)
    .threePointArc((-m2[0], m2[1]), (-Mx, My))
    .threePointArc((-m1[0], m1[1]), (-hw, Y_T1))
    .close()
    .extrude(-(ZB - R2 - 10.0) + H1)
)

arm = side.intersect(plan)

# ---------------- top boss ----------------
# (seam of the cylindrical face turned to +Y, where the arm covers it)
top_boss = cq.Workplane("XY").add(
    cq.Solid.makeCylinder(R1, H1, cq.Vector(0, 0, -H1 / 2.0), cq.Vector(0, 0, 1))
    .rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), 90)
)

body = top_boss.union(arm)

# fillet the vertical root edges where the arm sides meet the top boss
y_root = math.sqrt(R1 ** 2 - hw ** 2)
body = body.edges(
    cq.selectors.BoxSelector((-hw - 0.5, y_root - 0.5, -TH), (hw + 0.5, y_root + 0.5, TH))
).fillet(R_ROOT)

# ---------------- bores ----------------
bore1 = (
    cq.Solid.makeCylinder(D1_HOLE / 2.0, 2 * H1, cq.Vector(0, 0, -H1), cq.Vector(0, 0, 1))
    .rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), 45)
)
b2c = cq.Vector(0, YB + BORE2_DY, ZB + BORE2_DZ)
bore2 = (
    cq.Solid.makeCylinder(D2_HOLE / 2.0, 2 * L2, b2c - cq.Vector(L2, 0, 0), cq.Vector(1, 0, 0))
    .rotate(b2c, b2c + cq.Vector(1, 0, 0), 35)
)

result = body.cut(bore1).cut(bore2)

VIEW = {"azimuth": 45, "elevation": 26}
